import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 100.0                 # outer diameter of each disc
R = D / 2.0
T_FLANGE = 7.3            # thickness of top and bottom flanges
H_GROOVE = 4.3            # height of the central groove
TAPER = 2.0               # radial taper of each flange's outer face
R_HUB = 43.0              # radius of the groove floor (hub)
HOLE_D = 19.5             # diameter of the six through holes
HOLE_PCR = 23.6           # radius of the hole pattern
N_HOLES = 6
SLOT_L = 15.0             # centre slot length
SLOT_W = 4.6              # centre slot width
N_NOTCH = 12              # spherical notches around the groove lips
NOTCH_R = 4.4             # radius of each spherical notch
NOTCH_POS = 47.5          # radial position of the notch centres
PITCH = 110.0             # spacing of the 2 x 2 grid of discs
SEAM_ANGLE = -135.0       # where the revolve seam of the discs sits (deg)
HOLE_SEAM_ANGLE = 45.0    # where the seams of the hole walls sit (deg)

H = 2 * T_FLANGE + H_GROOVE


def make_disc():
    # half profile revolved around Z: bottom flange, groove, top flange
    pts = [
        (0, 0),
        (R, 0),
        (R - TAPER, T_FLANGE),
        (R_HUB, T_FLANGE),
        (R_HUB, T_FLANGE + H_GROOVE),
        (R - TAPER, T_FLANGE + H_GROOVE),
        (R, H),
        (0, H),
    ]
    body = (cq.Workplane("XZ").polyline(pts).close()
            .revolve(360, (0, 0, 0), (0, 1, 0))
            .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE))

    # six through holes on a hexagonal pattern (two on the X axis)
    hole = (cq.Workplane("XY").circle(HOLE_D / 2).extrude(H + 2)
            .translate((0, 0, -1))
            .rotate((0, 0, 0), (0, 0, 1), HOLE_SEAM_ANGLE))
    for i in range(N_HOLES):
        a = math.radians(i * 360.0 / N_HOLES)
        body = body.cut(hole.translate(
            (HOLE_PCR * math.cos(a), HOLE_PCR * math.sin(a), 0)))

    # rectangular centre slot along X
    slot = (cq.Workplane("XY").rect(SLOT_L, SLOT_W).extrude(H + 2)
            .translate((0, 0, -1)))
    body = body.cut(slot)

    # spherical notches cut into the lips of the groove
    zc = T_FLANGE + H_GROOVE / 2
    for i in range(N_NOTCH):
        a = math.radians(i * 360.0 / N_NOTCH)
        s = cq.Workplane("XY").sphere(NOTCH_R).translate(
            (NOTCH_POS * math.cos(a), NOTCH_POS * math.sin(a), zc))
        body = body.cut(s)
    return body


disc = make_disc()
solids = []
for ix in (-0.5, 0.5):
    for iy in (-0.5, 0.5):
        solids.extend(disc.translate((ix * PITCH, iy * PITCH, 0)).solids().vals())
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])

VIEW = {"azimuth": 45, "elevation": 26}
